import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# The wheel axis is X.  +X is the "show" face (fan spokes + hub cap),
# -X carries the hex drive and the set-screw boss.
R_OUT = 50.0          # tyre outer radius
W_TIRE = 41.0         # tyre width (along X)
R_RIM = 39.8          # tyre inner radius / rim outer radius
R_BORE = 33.7         # rim bore radius (spoke tips attach here)
W_RIM = 41.6          # rim width (protrudes a hair beyond the tyre faces)
F_TIRE = 3.2          # fillet on the tyre shoulders
F_LIP = 5.0           # rounded rim lip
SEAM_ANG = 240.0      # where the revolve seam of the tyre sits (cosmetic)

# hub
R_CAP = 11.8          # +X hub cap cylinder radius
CAP_X0 = 3.5          # cap start
CAP_X1 = 11.0         # cap front face
F_CAP = 1.0           # rounding of the cap front edge
HEX_RC = 11.0         # hex core circumradius
HEX_ROT = 37.5        # hex vertex angle (deg from +Y toward +Z)
HEX_X0 = -16.5        # hex core -X end
R_BOSS = 7.6          # set-screw boss radius
BOSS_X0 = -W_TIRE / 2 - 11.4   # boss end face
CH_BOSS = 0.5         # chamfer on the boss end
R_AXLE = 3.1          # axle bore radius
R_SET = 2.4           # set-screw hole radius
SET_X = BOSS_X0 + 5.6 # set-screw hole position along X
SET_ANG = 27.0        # set-screw direction (deg from +Y toward +Z)

# fan spokes
N_BLADE = 7
BLADE_ANG0 = 96.0     # angular position of first spoke (deg from +Y toward +Z)
HALF_SPREAD = 14.7    # angular half width of a spoke (deg)
BLADE_X1 = 4.0        # spoke front face
T_BLADE = 8.0         # spoke depth (along X)
F_BLADE = 1.5         # rounding of the spoke front edges
F_BLADE_B = 1.0       # rounding of the spoke back edges
BLADE_R0 = 9.2        # spoke inner end (buried in the hub)
BLADE_R1 = R_BORE + 1.5   # spoke outer end (buried in the rim)


def xcyl(r, x0, x1):
    """Solid cylinder about the X axis from x0 to x1."""
    return cq.Workplane("YZ").workplane(offset=x0).circle(r).extrude(x1 - x0)


def polar(r, a_deg):
    a = math.radians(a_deg)
    return (r * math.cos(a), r * math.sin(a))


# ---------------- tyre + rim (one revolved profile) ----------------
# half cross-section in the (x, r) plane, revolved about the X axis
c45 = math.cos(math.radians(45.0))
xt, xr = W_TIRE / 2, W_RIM / 2
wheel = (
    cq.Workplane("XY")
    .moveTo(-xr, R_BORE + F_LIP)
    .lineTo(-xr, R_RIM)
    .lineTo(-xt, R_RIM)
    .lineTo(-xt, R_OUT - F_TIRE)
    .threePointArc((-xt + F_TIRE * (1 - c45), R_OUT - F_TIRE * (1 - c45)),
                   (-xt + F_TIRE, R_OUT))
    .lineTo(xt - F_TIRE, R_OUT)
    .threePointArc((xt - F_TIRE * (1 - c45), R_OUT - F_TIRE * (1 - c45)),
                   (xt, R_OUT - F_TIRE))
    .lineTo(xt, R_RIM)
    .lineTo(xr, R_RIM)
    .lineTo(xr, R_BORE + F_LIP)
    .threePointArc((xr - F_LIP * (1 - c45), R_BORE + F_LIP * (1 - c45)),
                   (xr - F_LIP, R_BORE))
    .lineTo(-xr + F_LIP, R_BORE)
    .threePointArc((-xr + F_LIP * (1 - c45), R_BORE + F_LIP * (1 - c45)),
                   (-xr, R_BORE + F_LIP))
    .close()
    .revolve(360.0, (0, 0, 0), (1, 0, 0))
    .rotate((0, 0, 0), (1, 0, 0), SEAM_ANG)   # park the revolve seam out of sight
)

# ---------------- fan spokes ----------------
# 7 sector-shaped spokes (radial side faces) with a flat front face,
# running from the hex core out into the rim bore.
blades = None
for i in range(N_BLADE):
    a0 = BLADE_ANG0 + i * 360.0 / N_BLADE
    a_lo, a_hi = a0 - HALF_SPREAD, a0 + HALF_SPREAD
    b = (
        cq.Workplane("YZ").workplane(offset=BLADE_X1 - T_BLADE)
        .moveTo(*polar(BLADE_R0, a_lo))
        .lineTo(*polar(BLADE_R1, a_lo))
        .threePointArc(polar(BLADE_R1, a0), polar(BLADE_R1, a_hi))
        .lineTo(*polar(BLADE_R0, a_hi))
        .threePointArc(polar(BLADE_R0, a0), polar(BLADE_R0, a_lo))
        .close()
        .extrude(T_BLADE)
    )
    # round the radial edges of the front and back faces of each spoke
    b = b.faces(">X").edges("not %CIRCLE").fillet(F_BLADE)
    b = b.faces("<X").edges("not %CIRCLE").fillet(F_BLADE_B)
    blades = b if blades is None else blades.union(b)

# ---------------- hub ----------------
hexcore = (
    cq.Workplane("YZ").workplane(offset=HEX_X0)
    .transformed(rotate=(0, 0, HEX_ROT))
    .polygon(6, 2 * HEX_RC)
    .extrude(CAP_X0 - HEX_X0)
)
cap = xcyl(R_CAP, CAP_X0, CAP_X1).faces(">X").edges().fillet(F_CAP)
boss = xcyl(R_BOSS, BOSS_X0, HEX_X0 + 0.5).faces("<X").edges().chamfer(CH_BOSS)

hub = hexcore.union(cap).union(boss)

result = wheel.union(blades).union(hub)

# axle bore
result = result.cut(xcyl(R_AXLE, BOSS_X0 - 1, CAP_X1 + 1))

# set-screw cross hole through the boss
sa = math.radians(SET_ANG)
setscrew = (
    cq.Workplane(cq.Plane(origin=(SET_X, 0, 0), xDir=(1, 0, 0),
                          normal=(0, math.cos(sa), math.sin(sa))))
    .circle(R_SET).extrude(R_BOSS + 2, both=True)
)
result = result.cut(setscrew)
